"""Tilted tray / stand: a 7 deg inclined rim plate with a stepped pocket, a
through window split by a chevron rib, small pads with holes, a cable slot
through the back wall, sitting on a front foot and an inset wedge body."""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 250.0          # overall length (X)
W = 100.0          # overall depth in plan (Y)
TILT = 7.0         # inclination of the top plate (deg), rises toward the back
H_FRONT = 12.3     # height of the front top edge above the ground
T_RIM = 9.3        # thickness of the tilted rim plate (side reveal line)
R_CORNER = 4.5     # plan corner radius of the outer outline
R_TOP = 1.0        # fillet on the outer top edge
R_BOT = 1.2        # fillet on the outer bottom edge

# foot at the front (full width, reaches the ground)
FOOT_GROUND_Y = -31.4   # where the foot's rear edge meets the ground
FOOT_ANGLE = 45.0       # slope of the foot's rear edge (deg from horizontal)
FOOT_R = 5.0            # rounding where the foot meets the plate underside

# lower body (wedge under the plate, inset from the ends)
INSET = 4.5
LB_BACK_ANGLE = 38.0    # rear face inclination from vertical (deg)
LB_FILLET = 10.0        # rounding between rear face and ground

# pocket (plan coordinates)
PK_BACK = 30.6
PK_FRONT = -43.3
PK_STEP = -21.1
PK_XB = 118.5
PK_XF = 106.0
PK_DEPTH = 10.3
PK_R = 2.5

# back-right notch in the pocket back wall
BN_X0, BN_X1, BN_DEPTH_Y = 95.2, 112.7, 3.7
BN_R = 1.5

# lowered region behind the bridge
LN_X0, LN_X1 = -71.6, -44.8
LN_EXTRA = 2.0

# through opening
OP_X = 97.3
OP_Y0, OP_Y1 = -22.5, 13.2
OP_R = 12.0

# chevron bridge
BR_DEPTH = 12.8      # depth of the rib top below the top surface
BR_L_TOP, BR_L_APEX = -53.8, -41.6     # lobe side boundary
BR_R_TOP, BR_R_APEX, BR_R_BOT = -43.8, -33.8, -42.8   # main opening side boundary
BR_APEX_Y = -4.5
BR_R = 2.0

# tabs at the opening ends
TAB_LEN = 5.7
TAB_Y0, TAB_Y1 = -10.0, 0.7
TAB_R = 1.2
TAB_EXTRA = 1.5
TAB_HOLE_D = 1.8
TAB_HOLE_X = 100.4
TAB_HOLE_YS = (-2.2, -7.1)

# corner holes
HOLE_D = 2.4
HOLE_DEPTH = 30.0   # through (rear ones exit under the rim overhang)
HOLE_CB_D = 4.2     # bore from below
HOLE_CB_TOP = 2.0   # material left above the bore
HOLES = [(-121.8, 30.4), (121.8, 30.4), (-117.6, -43.3), (117.6, -43.3)]

# cable slot through the back wall
SL_X0, SL_X1 = -65.5, -49.3
SL_H = 6.5
SL_LIFT = 0.3        # slot floor above the lowered floor
SL_R = 1.5
WIN_TOP, WIN_BOT = 2.2, 13.2   # window recess in the back face (depth below top)
WIN_DEPTH = 6.0
WIN_X0, WIN_X1 = -68.8, -46.9

# ---------------- derived ----------------
th = math.radians(TILT)
s, c = math.sin(th), math.cos(th)
Y_F = -W / 2.0
LP = (W - T_RIM * s) / c           # plate length along the slope


def vloc(Y):
    """plan Y of a point on the top surface -> local slope coordinate"""
    return (Y - Y_F) / c


# key points of the side profile (Y, Z)
A = (Y_F, H_FRONT)                                   # front top edge
F = (Y_F + LP * c, H_FRONT + LP * s)                 # back top edge
E = (F[0] + T_RIM * s, F[1] - T_RIM * c)             # back edge of plate underside
B = (Y_F + H_FRONT * math.tan(th), 0.0)              # front bottom edge


def z_plate_bottom(Y):
    return E[1] - (E[0] - Y) * math.tan(th)


TOP = cq.Plane(origin=(0, Y_F, H_FRONT), xDir=(1, 0, 0), normal=(0, -s, c))
NDIR = cq.Vector(0, -s, c)


def wp(offset=0.0):
    return cq.Workplane(TOP).workplane(offset=offset)


def prism_poly(pts_plan, top_off, depth, r=None):
    """prism in the plate frame from plan (X,Y) points, from w=top_off down by depth"""
    pts = [(x, vloc(y)) for x, y in pts_plan]
    solid = wp(top_off).polyline(pts).close().extrude(-depth)
    if r:
        solid = solid.edges(cq.selectors.ParallelDirSelector(NDIR)).fillet(r)
    return solid


def prism_rect(x0, x1, y0, y1, top_off, depth, r=None):
    return prism_poly([(x0, y0), (x1, y0), (x1, y1), (x0, y1)], top_off, depth, r)


def fillet_corner(p_prev, p, p_next, r):
    """tangent points + arc midpoint for rounding corner p of a polyline"""
    def unit(a, b):
        d = math.hypot(b[0] - a[0], b[1] - a[1])
        return ((b[0] - a[0]) / d, (b[1] - a[1]) / d)
    u1 = unit(p, p_prev)
    u2 = unit(p, p_next)
    cosang = u1[0] * u2[0] + u1[1] * u2[1]
    ang = math.acos(max(-1.0, min(1.0, cosang)))
    t = r / math.tan(ang / 2.0)
    t1 = (p[0] + u1[0] * t, p[1] + u1[1] * t)
    t2 = (p[0] + u2[0] * t, p[1] + u2[1] * t)
    bis = (u1[0] + u2[0], u1[1] + u2[1])
    bl = math.hypot(*bis)
    bis = (bis[0] / bl, bis[1] / bl)
    dc = r / math.sin(ang / 2.0)
    ctr = (p[0] + bis[0] * dc, p[1] + bis[1] * dc)
    mid = (ctr[0] - bis[0] * r, ctr[1] - bis[1] * r)
    return t1, mid, t2


def rounded_wire(w, pts, radii):
    """closed wire on workplane w through pts, corners with radius>0 rounded by tangent arcs"""
    n = len(pts)
    segs = []
    for i in range(n):
        r = radii[i]
        if r and r > 0:
            segs.append(fillet_corner(pts[i - 1], pts[i], pts[(i + 1) % n], r))
        else:
            segs.append((pts[i], None, pts[i]))
    w = w.moveTo(*segs[0][2])
    for i in range(1, n + 1):
        t1, mid, t2 = segs[i % n]
        w = w.lineTo(*t1)
        if mid is not None:
            w = w.threePointArc(mid, t2)
    return w.close()


def rounded_profile(pts, radii, plane="YZ"):
    return rounded_wire(cq.Workplane(plane), pts, radii)


def prism_rounded(pts_plan, radii, top_off, depth):
    """rounded polygon prism in the plate frame (plan coordinates)"""
    pts = [(x, vloc(y)) for x, y in pts_plan]
    return rounded_wire(wp(top_off), pts, radii).extrude(-depth)


# ---------------- outer body ----------------
# rim + foot : rounded outline prism (perpendicular to plate) intersected with side profile
outline = (
    wp(0)
    .center(0, LP / 2.0)
    .rect(L, LP)
    .extrude(-40.0)
    .edges(cq.selectors.ParallelDirSelector(NDIR))
    .fillet(R_CORNER)
)

C = (FOOT_GROUND_Y, 0.0)
# foot rear edge rises at FOOT_ANGLE until it meets the plate underside
ta = math.tan(math.radians(FOOT_ANGLE))
# solve C.z + (y - C.y)*ta = z_plate_bottom(y)
m = math.tan(th)
zb0 = E[1] - E[0] * m
yD = (zb0 + C[0] * ta) / (ta - m)
D = (yD, z_plate_bottom(yD))

side = rounded_profile([A, F, E, D, C, B], [0, 0, 0, FOOT_R, 0, 0]).extrude(L / 2 + 5, both=True)
rim = outline.intersect(side)
rim = rim.faces(cq.selectors.DirectionMinMaxSelector(NDIR, True)).edges().fillet(R_TOP)

# lower body
G = (E[0] - E[1] * math.tan(math.radians(LB_BACK_ANGLE)), 0.0)
P0 = (C[0] - 6.0, 0.0)
P3 = (P0[0], z_plate_bottom(P0[0]))
lower = rounded_profile([P0, G, E, P3], [0, LB_FILLET, 0, 0]).extrude(L / 2 - INSET, both=True)

# soften the bottom edges, then merge
rim = rim.faces("<Z").edges().fillet(R_BOT)
lower = lower.faces("<Z").edges("|Y").fillet(R_BOT)
body = rim.union(lower, clean=True)

# ---------------- pocket ----------------
# main pocket outline incl. the small notch into the back wall (right)
pk_pts = [
    (-PK_XB, PK_BACK), (-PK_XB, PK_STEP), (-PK_XF, PK_STEP), (-PK_XF, PK_FRONT),
    (PK_XF, PK_FRONT), (PK_XF, PK_STEP), (PK_XB, PK_STEP), (PK_XB, PK_BACK),
    (BN_X1, PK_BACK), (BN_X1, PK_BACK + BN_DEPTH_Y), (BN_X0, PK_BACK + BN_DEPTH_Y), (BN_X0, PK_BACK),
]
pk_r = [PK_R] * 8 + [BN_R] * 4
body = body.cut(prism_rounded(pk_pts, pk_r, 2.0, PK_DEPTH + 2.0))

# lowered region behind the bridge
ln = prism_rect(LN_X0, LN_X1, OP_Y1 - 2.0, PK_BACK, -PK_DEPTH + 0.5, LN_EXTRA + 0.5)
body = body.cut(ln)

# through openings: lobe + main window separated by a chevron rib whose top sits
# below the pocket floor
body = body.cut(prism_rect(-OP_X, OP_X, OP_Y0, OP_Y1, 2.0, 2.0 + BR_DEPTH, OP_R))
lobe_pts = [(-OP_X, OP_Y1), (BR_L_TOP, OP_Y1), (BR_L_APEX, BR_APEX_Y), (BR_L_TOP, OP_Y0), (-OP_X, OP_Y0)]
body = body.cut(prism_rounded(lobe_pts, [OP_R, BR_R, BR_R, BR_R, OP_R], 2.0, 60.0))
main_pts = [(BR_R_TOP, OP_Y1), (OP_X, OP_Y1), (OP_X, OP_Y0), (BR_R_BOT, OP_Y0), (BR_R_APEX, BR_APEX_Y)]
body = body.cut(prism_rounded(main_pts, [BR_R, OP_R, OP_R, BR_R, BR_R], 2.0, 60.0))

# tabs (small recessed pads with two holes) at the opening ends
for sgn in (-1, 1):
    x_in = sgn * (OP_X - 3.0)
    x_out = sgn * (OP_X + TAB_LEN)
    tab_pts = [(x_in, TAB_Y0), (x_out, TAB_Y0), (x_out, TAB_Y1), (x_in, TAB_Y1)]
    if sgn > 0:
        tab_pts = [tab_pts[1], tab_pts[0], tab_pts[3], tab_pts[2]]
        rr = [TAB_R, 0, 0, TAB_R]
    else:
        rr = [0, TAB_R, TAB_R, 0]
    body = body.cut(prism_rounded(tab_pts, rr, -PK_DEPTH + 0.5, TAB_EXTRA + 0.5))
    xc = sgn * TAB_HOLE_X
    for yc in TAB_HOLE_YS:
        h = wp(-(PK_DEPTH + TAB_EXTRA) + 0.5).center(xc, vloc(yc)).circle(TAB_HOLE_D / 2).extrude(-6.0)
        body = body.cut(h)

# corner holes (perpendicular to the plate)
for (hx, hy) in HOLES:
    h = wp(2.0).center(hx, vloc(hy)).circle(HOLE_D / 2).extrude(-(2.0 + HOLE_DEPTH))
    body = body.cut(h)
    # wider bore from underneath, leaving a thin web under the top surface
    # (the rear bores stop at the rim underside so they do not groove the lower body)
    cb_len = HOLE_DEPTH if hy < 0 else T_RIM - HOLE_CB_TOP
    cb = wp(-HOLE_CB_TOP).center(hx, vloc(hy)).circle(HOLE_CB_D / 2).extrude(-cb_len)
    body = body.cut(cb)

# cable slot through the back wall (following the plate slope) opening into a
# taller window recess in the back face
SLOT_PLANE = cq.Plane(origin=(0, 0, 0), xDir=(1, 0, 0), normal=(0, -c, -s))


def slot_box(x0, x1, height, length, v_start, w_center, r):
    """box along the plate slope: X-range, height along plate normal, from v_start backwards"""
    b = (
        cq.Workplane(SLOT_PLANE)
        .rect(x1 - x0, height)
        .extrude(-length)
        .edges(cq.selectors.ParallelDirSelector(cq.Vector(0, c, s)))
        .fillet(r)
    )
    org = cq.Vector((x0 + x1) / 2.0, Y_F + v_start * c - w_center * s,
                    H_FRONT + v_start * s + w_center * c)
    return b.translate(org)


sl_top = -(PK_DEPTH + LN_EXTRA) + SL_LIFT + SL_H
body = body.cut(slot_box(SL_X0, SL_X1, SL_H, 40.0, vloc(PK_BACK) - 3.0, sl_top - SL_H / 2.0, SL_R))
body = body.cut(slot_box(WIN_X0, WIN_X1, WIN_BOT - WIN_TOP, WIN_DEPTH + 10.0, LP - WIN_DEPTH,
                         -(WIN_TOP + WIN_BOT) / 2.0, SL_R))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
